import cadquery as cq

# ------------------------------------------------------------------
# Desk set-up: open laptop, open-backed display housing, flat USB hub,
# power brick, two small plugs and the round cables joining them.
# All layout numbers are in grid units and scaled by U to millimetres.
#   X : left -> right, Y : lid back -> keyboard front, Z : up
# ------------------------------------------------------------------
U = 4.0  # mm per grid unit

# ---- laptop -------------------------------------------------------
LAP_W = 81.0          # width (X)
LAP_D = 54.3          # base depth (Y)
BASE_T = 2.7          # base thickness
LID_T = 2.9           # lid thickness
LID_H = 56.75         # lid height (from base bottom)
BASE_R = 1.5          # vertical corner radius at the front of the base
TRAY_SIDE = 3.3       # keyboard tray rim on the left / right
TRAY_NEAR = 8.3       # tray start (Y) measured from the lid back
TRAY_FAR = 3.0        # rim at the front edge
TRAY_DEPTH = 1.0
PAD_X0, PAD_X1 = 29.8, 53.4     # raised pad on the inner lid face
PAD_Z0, PAD_Z1 = 39.3, 51.3
PAD_H = 1.3
LAP_PORT_Z = 17.5     # port plug on the left side of the lid
LAP_PORT = (1.6, 2.5, 3.6)      # plug size: X, Y, Z

# ---- display housing (open-backed box) ---------------------------
BOX_X0, BOX_X1 = 148.5, 229.25
BOX_D = 40.3
BOX_Z0, BOX_Z1 = 4.25, 58.25
BOX_WALL = 3.7
BOX_PORT_Z = 39.75    # cable height at the housing
BOX_PORT_X1 = 159.5   # inner plug reaches to this X
BOX_PORT_H = 9.0      # inner plug height

# ---- hub / brick / small plugs -----------------------------------
HUB_X0, HUB_X1 = 28.1, 49.25
HUB_Z0, HUB_Z1 = 70.5, 84.35
HUB_Y0, HUB_Y1 = -0.1, 0.8
HUB_PORT_Z = 73.85    # laptop cable enters the hub side here
HUB_PORT_R = 1.05
HUB_PORT_L = 2.6
HUB_BOSS_X, HUB_BOSS_Z = 30.9, 73.4   # round socket boss on the back of the hub
HUB_BOSS_R, HUB_BOSS_H = 1.7, 1.3

BRICK_X0, BRICK_X1 = 13.0, 24.25
BRICK_Z0, BRICK_Z1 = 97.9, 105.1
BRICK_Y0, BRICK_Y1 = 0.2, 5.7
BRICK_R = 0.7

PLUG_A = (54.5, 60.3, 104.4, 107.5)     # x0, x1, z0, z1
PLUG_B = (54.5, 59.1, 92.2, 95.5)
PLUG_Y0, PLUG_Y1 = -0.1, 1.6
PLUG_R = 0.6

# ---- cables -------------------------------------------------------
CABLE_R = 0.66        # main (laptop / display) cables
CABLE_R2 = 0.38       # thin accessory cables
YC = 0.3              # cable plane (Y)
RISER_X = (36.5, 39.3, 42.8, 45.4)   # risers on top of the hub: brick, A, B, display
LAP_DROP_X = -8.25    # laptop cable runs down left of the lid
DISP_RUN_Z = 87.75    # display cable horizontal run height
DISP_DROP_X = 144.3   # display cable drops next to the housing
DISP_BACK_Y = 41.4    # ... then runs behind the open back of the housing


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box((x1 - x0) * U, (y1 - y0) * U, (z1 - z0) * U, centered=False)
            .translate((x0 * U, y0 * U, z0 * U)))


def cable(points, r=CABLE_R):
    """Round cable swept along a poly-line (points in grid units)."""
    pts = [cq.Vector(p[0] * U, p[1] * U, p[2] * U) for p in points]
    path = cq.Workplane("XY").polyline([(p.x, p.y, p.z) for p in pts])
    d = (pts[1] - pts[0]).normalized()
    # keep the profile seam on the hidden (+Y) side of the cable
    xdir = cq.Vector(0, 1, 0) if abs(d.y) < 0.9 else cq.Vector(0, 0, 1)
    plane = cq.Plane(origin=pts[0], xDir=xdir, normal=d)
    prof = cq.Workplane(plane).circle(r * U)
    return prof.sweep(path, transition="right")


# ================= laptop =================
base = box(0, LAP_W, 0, LAP_D, 0, BASE_T)
base = base.edges("|Z").edges(">Y").fillet(BASE_R * U)
tray = box(TRAY_SIDE, LAP_W - TRAY_SIDE, TRAY_NEAR, LAP_D - TRAY_FAR,
           BASE_T - TRAY_DEPTH, BASE_T + 1)
base = base.cut(tray)

lid = box(0, LAP_W, 0, LID_T, 0, LID_H)
pad = box(PAD_X0, PAD_X1, LID_T - 0.1, LID_T + PAD_H, PAD_Z0, PAD_Z1)
lid = lid.union(pad)
laptop = base.union(lid)

lap_plug = (box(-LAP_PORT[0], 0.05, 0.2, 0.2 + LAP_PORT[1],
                LAP_PORT_Z - LAP_PORT[2] / 2, LAP_PORT_Z + LAP_PORT[2] / 2)
            .edges("|Y").fillet(0.4 * U))
laptop = laptop.union(lap_plug)

# ================= display housing =================
housing = (box(BOX_X0, BOX_X1, 0, BOX_D, BOX_Z0, BOX_Z1)
           .faces(">Y").shell(-BOX_WALL * U))
housing_plug = (box(BOX_X0 + BOX_WALL - 0.05, BOX_PORT_X1, BOX_D - 3.3, BOX_D - 0.1,
                    BOX_PORT_Z - BOX_PORT_H / 2, BOX_PORT_Z + BOX_PORT_H / 2)
                .edges("|Y").fillet(1.0 * U))
housing = housing.union(housing_plug)

# ================= hub, brick, small plugs =================
hub = box(HUB_X0, HUB_X1, HUB_Y0, HUB_Y1, HUB_Z0, HUB_Z1).edges("|Y").fillet(0.25 * U)
hub_plug = (cq.Workplane("YZ").circle(HUB_PORT_R * U).extrude(HUB_PORT_L * U)
            .translate(((HUB_X0 - HUB_PORT_L + 0.05) * U, YC * U, HUB_PORT_Z * U)))
hub = hub.union(hub_plug)
hub_boss = (cq.Workplane("XZ", origin=(0, HUB_Y1 * U, 0))
            .center(HUB_BOSS_X * U, HUB_BOSS_Z * U)
            .circle(HUB_BOSS_R * U).extrude(-(HUB_BOSS_H + 0.05) * U)
            .translate((0, -0.05 * U, 0))
            .faces(">Y").edges().fillet(0.5 * U))
hub = hub.union(hub_boss)

brick = box(BRICK_X0, BRICK_X1, BRICK_Y0, BRICK_Y1, BRICK_Z0, BRICK_Z1).edges().fillet(BRICK_R * U)

plug_a = box(PLUG_A[0], PLUG_A[1], PLUG_Y0, PLUG_Y1, PLUG_A[2], PLUG_A[3]).edges().fillet(PLUG_R * U)
plug_b = box(PLUG_B[0], PLUG_B[1], PLUG_Y0, PLUG_Y1, PLUG_B[2], PLUG_B[3]).edges().fillet(PLUG_R * U)

# ================= cables =================
hub_top = HUB_Z1 - 0.1
brick_z = (BRICK_Z0 + BRICK_Z1) / 2
a_z = (PLUG_A[2] + PLUG_A[3]) / 2
b_z = (PLUG_B[2] + PLUG_B[3]) / 2
c_lap = cable([(HUB_X0 - HUB_PORT_L + 0.1, YC, HUB_PORT_Z), (LAP_DROP_X, YC, HUB_PORT_Z),
               (LAP_DROP_X, YC, LAP_PORT_Z), (-LAP_PORT[0] + 0.1, YC, LAP_PORT_Z)])
c_brick = cable([(BRICK_X1 - 1.5, YC, brick_z), (RISER_X[0], YC, brick_z),
                 (RISER_X[0], YC, hub_top)], r=CABLE_R2)
c_a = cable([(RISER_X[1], YC, hub_top), (RISER_X[1], YC, a_z), (PLUG_A[0] + 0.1, YC, a_z)], r=CABLE_R2)
c_b = cable([(RISER_X[2], YC, hub_top), (RISER_X[2], YC, b_z), (PLUG_B[0] + 0.1, YC, b_z)], r=CABLE_R2)
disp_end_x = BOX_PORT_X1 - 2.2
c_disp = cable([(RISER_X[3], YC, hub_top), (RISER_X[3], YC, DISP_RUN_Z),
                (DISP_DROP_X, YC, DISP_RUN_Z), (DISP_DROP_X, YC, BOX_PORT_Z),
                (DISP_DROP_X, DISP_BACK_Y, BOX_PORT_Z), (disp_end_x, DISP_BACK_Y, BOX_PORT_Z),
                (disp_end_x, BOX_D - 0.3, BOX_PORT_Z)])

result = (laptop.union(housing).union(hub).union(brick).union(plug_a).union(plug_b)
          .union(c_lap).union(c_brick).union(c_a).union(c_b).union(c_disp))

VIEW = {"azimuth": 45, "elevation": 26}
